import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Keyboard-style bottom case / tray with raised gasket plate (all mm)
# ---------------------------------------------------------------------------
HX = 190.0            # half length of the body (X)
HY = 67.2             # half depth of the rectangular part (Y)
XC = -7.0             # X position of the chevron centre
BACK_HALF = 103.5     # half span of the back V notch
V_DEPTH = 15.0        # depth of the back V notch
FRONT_HALF = 105.3    # half span of the front trapezoid bulge
FRONT_FLAT_HALF = 19.4
FRONT_PROT = 11.8     # how far the front bulge sticks out
CORNER_R = 8.3        # outer plan-view corner radius
R_BREAK = 60.0        # blend radius at the chevron break points
R_APEX = 5.0          # radius at the apex of the back V

FLANGE_W = 10.6       # width of the screw flange around the raised plate
PLATE_CORNER_R = 6.5  # plan-view corner radius of the raised plate
PLATE_H = 4.0         # height of raised plate above the flange
PLATE_CHAMFER = 0.6   # chamfer on the top edge of the plate

T_FRONT = 5.2         # flange thickness at the front-most point
TILT_DEG = 5.0        # typing angle of the bottom face

HOLE_D = 3.8
CSK_D = 6.8           # countersink on the underside
HOLE_X = [-172.8, -100.2, -26.3, 26.3, 100.2, 172.8]

TAB_R = 4.2           # half width of the tabs on the plate
TAB_GAP = 1.0         # clearance tab tip -> outer edge
TAB_FILLET = 4.0      # fillet at the root of the tabs
TABS_BACK_X = [-160.0, -48.3, 37.0, 134.6]
TABS_FRONT_X = [-135.7, -50.2, 37.9, 134.6]
TABS_SIDE_Y = [-31.0, 31.0]

NOTCH_XC = -141.2     # cable notch in the back edge of the plate
NOTCH_W = 14.8
NOTCH_D = 10.6
NOTCH_BELOW = 3.0     # pocket floor depth below the flange top

FOOT_XC = 137.6       # bottom rubber foot pockets (4x)
FOOT_L = 41.0
FOOT_W = 6.0
FOOT_DEPTH = 2.5

# ---------------------------------------------------------------------------
# plan-view outline (CCW)
# ---------------------------------------------------------------------------
outer_pts = [
    (-HX, -HY),
    (XC - FRONT_HALF, -HY),
    (XC - FRONT_FLAT_HALF, -HY - FRONT_PROT),
    (XC + FRONT_FLAT_HALF, -HY - FRONT_PROT),
    (XC + FRONT_HALF, -HY),
    (HX, -HY),
    (HX, HY),
    (XC + BACK_HALF, HY),
    (XC, HY - V_DEPTH),
    (XC - BACK_HALF, HY),
    (-HX, HY),
]
Y_FRONT = -HY - FRONT_PROT


def poly_wire(pts):
    return cq.Wire.makePolygon([cq.Vector(x, y, 0) for x, y in pts], close=True)


def offset_polygon(pts, d):
    """Offset a CCW polygon inwards by d (sharp corners)."""
    n = len(pts)
    lines = []
    for i in range(n):
        (x0, y0), (x1, y1) = pts[i], pts[(i + 1) % n]
        L = math.hypot(x1 - x0, y1 - y0)
        nx, ny = -(y1 - y0) / L, (x1 - x0) / L      # inward normal
        lines.append(((x0 + nx * d, y0 + ny * d), (x1 - x0, y1 - y0)))
    out = []
    for i in range(n):
        (p, u), (q, v) = lines[i - 1], lines[i]
        den = u[0] * v[1] - u[1] * v[0]
        t = ((q[0] - p[0]) * v[1] - (q[1] - p[1]) * v[0]) / den
        out.append((p[0] + t * u[0], p[1] + t * u[1]))
    return out


def is_convex(pts, i):
    n = len(pts)
    a, b, c = pts[i - 1], pts[i], pts[(i + 1) % n]
    return (b[0] - a[0]) * (c[1] - b[1]) - (b[1] - a[1]) * (c[0] - b[0]) > 0


def rounded_face(pts, radii):
    """Planar face from polygon with per-vertex 2D fillets (radius 0 = sharp)."""
    face = cq.Face.makeFromWires(poly_wire(pts))
    groups = {}
    for p, r in zip(pts, radii):
        if r > 0:
            groups.setdefault(round(r, 4), []).append(p)
    for r, plist in groups.items():
        verts = [v for v in face.Vertices()
                 if any(abs(v.X - x) < 1e-4 and abs(v.Y - y) < 1e-4 for x, y in plist)]
        face = face.fillet2D(r, verts)
    return face


corner_idx = {0, 5, 6, 10}
outer_r = []
inner_r = []
for i in range(len(outer_pts)):
    if i in corner_idx:
        outer_r.append(CORNER_R)
        inner_r.append(PLATE_CORNER_R)
    else:
        rb = R_APEX if i == 8 else R_BREAK
        outer_r.append(rb)
        inner_r.append(rb - FLANGE_W if is_convex(outer_pts, i) else rb + FLANGE_W)

outer_face = rounded_face(outer_pts, outer_r)
inner_pts = offset_polygon(outer_pts, FLANGE_W)
inner_face = rounded_face(inner_pts, inner_r)


def edge_point(x, side):
    """Point on the outer outline at given X on back (+1) or front (-1) side,
    plus the outward unit normal."""
    n = len(outer_pts)
    best = None
    for i in range(n):
        (x0, y0), (x1, y1) = outer_pts[i], outer_pts[(i + 1) % n]
        if abs(x1 - x0) < 1e-9:
            continue
        if min(x0, x1) - 1e-9 <= x <= max(x0, x1) + 1e-9:
            ym = 0.5 * (y0 + y1)
            if (side > 0 and ym > 0) or (side < 0 and ym < 0):
                t = (x - x0) / (x1 - x0)
                y = y0 + t * (y1 - y0)
                dx, dy = x1 - x0, y1 - y0
                L = math.hypot(dx, dy)
                # CCW polygon -> outward normal is (dy, -dx)
                nx, ny = dy / L, -dx / L
                best = (x, y, nx, ny)
    return best


tab_defs = []
for x in TABS_BACK_X:
    tab_defs.append(edge_point(x, +1))
for x in TABS_FRONT_X:
    tab_defs.append(edge_point(x, -1))
for y in TABS_SIDE_Y:
    tab_defs.append((-HX, y, -1.0, 0.0))
    tab_defs.append((HX, y, 1.0, 0.0))

# ---------------------------------------------------------------------------
# raised plate with tabs
# ---------------------------------------------------------------------------
plate = cq.Workplane("XY").add(cq.Solid.extrudeLinear(inner_face, cq.Vector(0, 0, PLATE_H)))
junctions = []
for (px, py, nx, ny) in tab_defs:
    tip = (px - nx * (TAB_GAP + TAB_R), py - ny * (TAB_GAP + TAB_R))
    base = (px - nx * (FLANGE_W + 4.0), py - ny * (FLANGE_W + 4.0))
    mx, my = 0.5 * (tip[0] + base[0]), 0.5 * (tip[1] + base[1])
    length = math.hypot(tip[0] - base[0], tip[1] - base[1]) + 2 * TAB_R
    ang = math.degrees(math.atan2(ny, nx))
    tab = (cq.Workplane("XY").center(mx, my)
           .slot2D(length, 2 * TAB_R, ang).extrude(PLATE_H))
    plate = plate.union(tab)
    # root points (where tab flanks meet the plate edge)
    tx, ty = -ny, nx
    rx, ry = px - nx * FLANGE_W, py - ny * FLANGE_W
    junctions.append((rx + tx * TAB_R, ry + ty * TAB_R))
    junctions.append((rx - tx * TAB_R, ry - ty * TAB_R))

plate = plate.clean()


class NearPoints(cq.Selector):
    def __init__(self, pts, tol):
        self.pts = pts
        self.tol = tol

    def filter(self, objs):
        out = []
        for o in objs:
            c = o.Center()
            for (x, y) in self.pts:
                if math.hypot(c.x - x, c.y - y) < self.tol:
                    out.append(o)
                    break
        return out


plate = plate.edges("|Z").edges(NearPoints(junctions, 1.0)).fillet(TAB_FILLET)

# small chamfer around the top edge of the raised plate
plate = plate.faces(">Z").edges().chamfer(PLATE_CHAMFER)

# ---------------------------------------------------------------------------
# wedge shaped base flange
# ---------------------------------------------------------------------------
a = math.radians(TILT_DEG)
up = (0, math.sin(a), math.cos(a))        # normal of the sloped bottom (into part)


def bottom_z(y):
    """Z of the sloped underside at a given Y."""
    return -T_FRONT - (y - Y_FRONT) * math.tan(a)


base = cq.Workplane("XY").add(
    cq.Solid.extrudeLinear(outer_face, cq.Vector(0, 0, -40.0)))
bottom_plane = cq.Plane(origin=(0, Y_FRONT, -T_FRONT), xDir=(1, 0, 0), normal=up)
cutter = cq.Workplane(bottom_plane).rect(1000, 1000).extrude(-100)
base = base.cut(cutter)

body = base.union(plate)

# half-pipe cable channel at the back edge of the plate (sunk below flange top)
notch_back_y = HY - FLANGE_W
notch_r = NOTCH_W / 2
notch = cq.Workplane("XY").add(cq.Solid.makeCylinder(
    notch_r, NOTCH_D,
    pnt=cq.Vector(NOTCH_XC, notch_back_y - NOTCH_D, -NOTCH_BELOW + notch_r),
    dir=cq.Vector(0, 1, 0)))
body = body.cut(notch)

# ---------------------------------------------------------------------------
# screw holes along the flange centre-line
# ---------------------------------------------------------------------------
hole_pts = []
for x in HOLE_X:
    for side in (+1, -1):
        px, py, nx, ny = edge_point(x, side)
        hole_pts.append((px - nx * FLANGE_W / 2, py - ny * FLANGE_W / 2))
holes = (cq.Workplane("XY").workplane(offset=-40)
         .pushPoints(hole_pts).circle(HOLE_D / 2).extrude(50))
body = body.cut(holes)

# 90 deg countersinks from the underside
for (hx, hy) in hole_pts:
    zb = bottom_z(hy)
    h = CSK_D / 2 + 1.0
    cone = cq.Solid.makeCone(CSK_D / 2 + 1.0, 0.0, h,
                             pnt=cq.Vector(hx, hy, zb - 1.0),
                             dir=cq.Vector(0, 0, 1))
    body = body.cut(cq.Workplane("XY").add(cone))

# ---------------------------------------------------------------------------
# foot pockets in the sloped bottom
# ---------------------------------------------------------------------------
for sx in (-1, 1):
    for sy in (-1, 1):
        fx = sx * FOOT_XC
        fy = sy * (HY - FLANGE_W / 2)
        pl = cq.Plane(origin=(fx, fy, bottom_z(fy)), xDir=(1, 0, 0), normal=up)
        pocket = (cq.Workplane(pl).workplane(offset=-2.0)
                  .slot2D(FOOT_L, FOOT_W, 0).extrude(FOOT_DEPTH + 2.0))
        body = body.cut(pocket)

result = body.clean()

VIEW = {"azimuth": 45, "elevation": 26}
